"""Obround cover / retainer plate with three through holes.

A stadium-shaped (obround) cap: a 3 mm top plate with a 3 mm skirt wall around the
whole perimeter, open underneath.  The top carries two large keyhole openings
(round hole + radial notch, 180 deg rotationally symmetric) near the ends and a
plain round hole in the middle.  The outer top edge is filleted.
"""
import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # overall length (X)
W = 40.0           # overall width (Y) -> end radius W/2
H = 14.75          # overall height (Z)
WALL = 3.0         # skirt wall thickness
TOP = 3.0          # top plate thickness
R_TOP = 1.25       # fillet on the outer top edge

D_BIG = 30.0       # large end holes
X_BIG = 41.6       # large hole centres at x = +/- X_BIG
D_MID = 22.0       # centre hole (at the origin)

NOTCH_W = 9.0      # keyhole notch width (full-round end)
NOTCH_LEN = 19.7   # big-hole centre -> notch end-arc centre
NOTCH_ANG = 32.0   # notch direction of the -X hole (deg from +X); +X hole is rotated 180 deg

# ---------------- body: obround cap, open at the bottom ----------------
body = cq.Workplane("XY").slot2D(L, W).extrude(H)
body = body.edges(">Z").fillet(R_TOP)

cavity = (
    cq.Workplane("XY")
    .slot2D(L - 2.0 * WALL, W - 2.0 * WALL)
    .extrude(H - TOP)
)
body = body.cut(cavity)


# ---------------- through-cut tools ----------------
def through(wp):
    """Extrude a 2D profile straight through the whole part height."""
    return wp.extrude(H + 2.0).translate((0, 0, -1.0))


def keyhole(cx, ang_deg):
    """Round hole at (cx, 0) plus a radial full-round notch pointing at ang_deg."""
    a = math.radians(ang_deg)
    hole = through(cq.Workplane("XY").center(cx, 0).circle(D_BIG / 2.0))
    # the slot runs from the hole centre to the notch end-arc centre
    mx = cx + 0.5 * NOTCH_LEN * math.cos(a)
    my = 0.5 * NOTCH_LEN * math.sin(a)
    notch = through(
        cq.Workplane("XY")
        .center(mx, my)
        .slot2D(NOTCH_LEN + NOTCH_W, NOTCH_W, ang_deg)
    )
    return hole.union(notch)


cutter = keyhole(-X_BIG, NOTCH_ANG).union(keyhole(X_BIG, NOTCH_ANG + 180.0))
cutter = cutter.union(through(cq.Workplane("XY").circle(D_MID / 2.0)))

result = body.cut(cutter)

VIEW = {"azimuth": 45, "elevation": 26}
